import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# plate (origin on the stud axis, plate bottom at z = 0, +Y = back)
PLATE_W = 38.0          # overall width of the wide (front) section
PLATE_D = 38.0          # overall depth front-to-back
PLATE_T = 3.2           # plate thickness
NARROW_W = 33.3         # width of the narrower back section
STEP_FROM_BACK = 22.15  # distance from back edge to the width step
STUD_FROM_BACK = 14.2   # distance from back edge to stud axis
BACK_R = 4.4            # back corner radius
STEP_R = 2.35           # convex corner radius of the wide section at the step
NOTCH_W = 15.85         # width of the front notch
NOTCH_D = 7.9           # depth of the front notch

# locating domes on the top face
DOME_R = 1.45
DOME_OFFSET = 7.1       # x / y offset of the 4 domes from the stud axis
DOME_POLE_ANGLE = 45.0  # direction of the (hidden) revolve poles on the base

# small blind hole on the underside at the back edge
UHOLE_D = 3.25
UHOLE_DEPTH = 1.6
UHOLE_INSET = UHOLE_D / 2.0 - 0.004   # centre distance from the back edge (just breaks through)

# stud: collar + 3/8"-16 style thread (modelled as plain rings)
COLLAR_R = 4.9
COLLAR_H = 4.8
FLAT_W_UP = 1.85        # width of the four flats, upper half of the collar
FLAT_W_LO = 1.72        # width of the four flats, lower half (slightly shallower)
THREAD_L = 9.15
R_MAJ = 4.76
R_ROOT = 3.85
PITCH = 1.5875
N_CREST = 5
FIRST_CREST = 1.15
CREST_FLAT = 0.12
R_TOP = 3.33
SEAM_ANGLE = 135.0      # where the thread run-out / revolve seam sits

# ---------------- plate ----------------
yb = STUD_FROM_BACK
yf = STUD_FROM_BACK - PLATE_D
ys = STUD_FROM_BACK - STEP_FROM_BACK
hw = PLATE_W / 2.0
nw = NARROW_W / 2.0
nhw = NOTCH_W / 2.0
yn = yf + NOTCH_D
V = cq.Vector


def arc_mid(cx, cy, r, ang_deg):
    a = math.radians(ang_deg)
    return V(cx + r * math.cos(a), cy + r * math.sin(a), 0)


def line(p, q):
    return cq.Edge.makeLine(V(p[0], p[1], 0), V(q[0], q[1], 0))


def arc(p, mid, q):
    return cq.Edge.makeThreePointArc(V(p[0], p[1], 0), mid, V(q[0], q[1], 0))


# outline, counter-clockwise from the front-left corner (lines + tangent arcs)
r2 = min(STEP_R, hw - nw)
chains = [
    [line((-hw, yf), (-nhw, yf))],
    [line((-nhw, yf), (-nhw, yn))],
    [line((-nhw, yn), (nhw, yn))],
    [line((nhw, yn), (nhw, yf))],
    [line((nhw, yf), (hw, yf))],
    # right side of the wide section + rounded corner at the step
    [line((hw, yf), (hw, ys - r2)),
     arc((hw, ys - r2), arc_mid(hw - r2, ys - r2, r2, 45), (hw - r2, ys))]
    + ([line((hw - r2, ys), (nw, ys))] if hw - r2 - nw > 1e-6 else []),
    # narrow back section: right side, back corners, back edge, left side
    [line((nw, ys), (nw, yb - BACK_R)),
     arc((nw, yb - BACK_R), arc_mid(nw - BACK_R, yb - BACK_R, BACK_R, 45), (nw - BACK_R, yb)),
     line((nw - BACK_R, yb), (-nw + BACK_R, yb)),
     arc((-nw + BACK_R, yb), arc_mid(-nw + BACK_R, yb - BACK_R, BACK_R, 135), (-nw, yb - BACK_R)),
     line((-nw, yb - BACK_R), (-nw, ys))],
    # left rounded corner at the step + left side of the wide section
    ([line((-nw, ys), (-hw + r2, ys))] if hw - r2 - nw > 1e-6 else [])
    + [arc((-hw + r2, ys), arc_mid(-hw + r2, ys - r2, r2, 135), (-hw, ys - r2)),
       line((-hw, ys - r2), (-hw, yf))],
]
edges = [e for ch in chains for e in ch]
outline_wire = cq.Wire.assembleEdges(edges)
plate_face = cq.Face.makeFromWires(outline_wire)
plate = cq.Workplane("XY").add(cq.Solid.extrudeLinear(plate_face, V(0, 0, PLATE_T)))

# domes
for sx in (-1, 1):
    for sy in (-1, 1):
        # hemisphere: half-disc in the plate plane revolved 180 deg about X,
        # so the seams/poles lie on the plate face
        dome = (
            cq.Workplane("XY")
            .moveTo(-DOME_R, 0)
            .threePointArc((0, DOME_R), (DOME_R, 0))
            .close()
            .revolve(180, (-1, 0, 0), (1, 0, 0))
            .rotate((0, 0, 0), (0, 0, 1), DOME_POLE_ANGLE)
            .translate((sx * DOME_OFFSET, sy * DOME_OFFSET, PLATE_T))
        )
        plate = plate.union(dome)

# underside blind hole near the back edge
uhole = (
    cq.Workplane("XY")
    .center(0, yb - UHOLE_INSET)
    .circle(UHOLE_D / 2.0)
    .extrude(UHOLE_DEPTH)
)
plate = plate.cut(uhole)

# ---------------- stud ----------------
z0 = PLATE_T
big = 20.0
collar = cq.Workplane("XY").workplane(offset=z0).circle(COLLAR_R).extrude(COLLAR_H)
# four shallow flats on the collar; the upper half is cut slightly deeper
for (zlo, zhi, w) in ((-1.0, COLLAR_H / 2.0, FLAT_W_LO),
                      (COLLAR_H / 2.0, COLLAR_H + 1.0, FLAT_W_UP)):
    d = math.sqrt(COLLAR_R ** 2 - (w / 2.0) ** 2)
    for ang in (0, 90, 180, 270):
        cutter = (
            cq.Workplane("XY")
            .box(big, big, zhi - zlo, centered=(False, True, False))
            .translate((d, 0, z0 + zlo))
            .rotate((0, 0, 0), (0, 0, 1), ang)
        )
        collar = collar.cut(cutter)

# thread section: revolved ring profile (r, z) relative to thread base
zt = z0 + COLLAR_H
flank = (R_MAJ - R_ROOT) * math.tan(math.radians(30))
pts = [(0.0, 0.0), (R_ROOT, 0.0)]
for k in range(N_CREST):
    zc = FIRST_CREST + k * PITCH
    pts.append((R_ROOT, zc - CREST_FLAT / 2.0 - flank))
    pts.append((R_MAJ, zc - CREST_FLAT / 2.0))
    pts.append((R_MAJ, zc + CREST_FLAT / 2.0))
    pts.append((R_ROOT, zc + CREST_FLAT / 2.0 + flank))
zlast = pts[-1][1]
pts.append((R_TOP, zlast + 0.15))
pts.append((R_TOP, THREAD_L))
pts.append((0.0, THREAD_L))

thread = (
    cq.Workplane("XZ")
    .polyline(pts)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
    .translate((0, 0, zt))
)

stud = collar.union(thread)
result = plate.union(stud)

VIEW = {"azimuth": 45, "elevation": 26}
